import cadquery as cq

# =====================================================================
# Hand-held clam-shell game console (DS-Lite style), opened 90 degrees.
#   * lower half stands upright: outer shell face toward -Y, controls
#     (screen, D-pad, ABXY, start/select) on the +Y face
#   * lid (screen half) lies flat on the table, extending toward +Y
#   * hinge barrel along X at the foot of the upright half
# Units: mm.  X = width, Y = depth, Z = height.
# =====================================================================

# ---------------- overall ----------------
W = 133.0            # width of both halves (X)
T = 13.2             # thickness of the upright half (Y)
H = 73.8             # height of the upright half (Z)
R_XZ = 3.7           # corner radius of the upright, front view
R_OUT = 4.6          # rounding of the outer (-Y) face edges
R_IN = 0.6           # rounding of the inner (+Y) face edges

# ---------------- hinge ----------------
HB_D = 8.3           # barrel depth beyond the inner face
HB_H = 10.6          # barrel height
HB_R_TOP = 4.9       # top/back rounding of the barrel profile
HB_R_BOT = 2.4       # bottom/back rounding of the end knuckles
HB_SPLIT = 45.0      # |X| of the split between knuckles and middle barrel
GROOVE = 0.5         # width of separation grooves
KN_END_R = 3.5       # rounding of the knuckle outer ends

# ---------------- lid ----------------
LID_T = 5.2          # lid thickness
LID_Y1 = 85.3        # far end of the lid
LID_R_CORNER = 3.4   # plan-view corner radius at the far end
LID_R_BOT = 4.5      # rounding of the lid's lower edges
LID_R_TOP = 0.6      # rounding of the rim's outer top edge
RIM_W = 2.8          # rim width (three sides, open toward the hinge)
RIM_DEPTH = 2.6      # depth of the tray inside the rim
FLOOR_FILLET = 0.9
SPK_X = (44.9, 50.7, 56.5)   # speaker hole columns (mirrored in X)
SPK_Y = (49.3, 54.9)         # speaker hole rows
SPK_D = 1.7

# ---------------- screens ----------------
SCR_W = 67.8
SCR_H = 50.8
SCR_DEPTH = 0.4
SCR_IN_Z = 39.9      # centre height of the screen on the upright half
SCR_LID_Y = 49.9     # centre of the screen on the lid

# ---------------- controls on the inner face ----------------
PAD_X, PAD_Z = -52.2, 35.3
PAD_LEN, PAD_ARM, PAD_H = 18.5, 6.2, 1.5
ABXY_X, ABXY_Z = 49.6, 34.6
ABXY_OFF, ABXY_R, ABXY_H = 8.5, 3.6, 2.2
SS_X, SS_Z = 41.0, (56.2, 64.4)     # start / select
SS_R, SS_H = 1.35, 1.9

# ---------------- top edge ----------------
GBA_X, GBA_HALF = 0.6, 31.9         # cartridge slot notch (top / outer edge)
GBA_Y, GBA_D = 7.3, 4.1
SCOOP_X, SCOOP_W, SCOOP_D = 0.9, 27.8, 5.2   # finger scoop below the notch
KEY_X, KEY_Y, KEY_R = 49.45, 4.95, 3.25       # stylus keyhole
KEY_SLOT_X0, KEY_SLOT_W, KEY_DEPTH = 40.6, 3.2, 3.0
SW_X0, SW_X1 = -51.06, -39.06                # power switch slot
SW_Y0, SW_Y1 = 4.9, 9.6
SW_KNOB_W, SW_KNOB_UP = 6.2, 3.0             # knob width and height above top
SW_PLATE_UP = 0.45                           # slider plate standing proud of the top

# ---------------- +X side ----------------
STRAP_X0, STRAP_ZC, STRAP_W, STRAP_END, STRAP_DEPTH = 56.4, 42.8, 5.3, 7.63, 1.6
VOL_Y = (5.14, 9.29)                 # volume slider pocket
VOL_Z = (18.6, 31.9)
VOL_KNOB_Z = (24.6, 31.5)
VOL_KNOB_X1 = 69.1                   # knob outer face
VOL_NUB_X1 = 71.26                   # triangular grip outer face

# ---------------- shoulder buttons (lower outer corners) ----------------
SH_X, SH_Y, SH_Z = 46.0, 8.6, 11.8

# ---------------- underside ----------------
CARD_X, CARD_Y, CARD_L, CARD_W = 1.7, 3.8, 34.8, 4.4
WIN_X, WIN_Y, WIN_L, WIN_W = -25.3, 6.7, 6.5, 2.8
LED_X, LED_Y, LED_S = (24.9, 31.3), 6.1, 1.3

hw = W / 2.0
LID_Y0 = T + HB_D    # visible start of the lid


def rounded_rect(wp, x0, x1, y0, y1, r00, r10, r11, r01):
    """Closed rounded rectangle on workplane wp (local coords).
    Radii at corners (x0,y0), (x1,y0), (x1,y1), (x0,y1); 0 = sharp."""
    w = wp.moveTo(x0 + r00, y0).lineTo(x1 - r10, y0)
    w = w.radiusArc((x1, y0 + r10), -r10) if r10 > 0 else w
    w = w.lineTo(x1, y1 - r11)
    w = w.radiusArc((x1 - r11, y1), -r11) if r11 > 0 else w
    w = w.lineTo(x0 + r01, y1)
    w = w.radiusArc((x0, y1 - r01), -r01) if r01 > 0 else w
    w = w.lineTo(x0, y0 + r00)
    w = w.radiusArc((x0 + r00, y0), -r00) if r00 > 0 else w
    return w.close()


def box_at(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# =====================================================================
# Upright half: rounded shell
# =====================================================================
upright = cq.Workplane("XY").box(W, T, H, centered=(True, False, False))
upright = upright.faces("<Y").edges().fillet(R_OUT)
upright = upright.edges("|Y").fillet(R_XZ)
upright = upright.faces(">Y").edges().fillet(R_IN)


# ---- hinge barrel: middle barrel + two end knuckles ----
def barrel(x0, x1, round_bottom):
    b = box_at(x0, x1, T - 1.0, T + HB_D, 0.0, HB_H)
    b = b.edges("|X").edges(">Y").edges(">Z").fillet(HB_R_TOP)
    if round_bottom:
        b = b.edges("|X").edges(">Y").edges("<Z").fillet(HB_R_BOT)
    return b


mid = barrel(-HB_SPLIT + GROOVE / 2, HB_SPLIT - GROOVE / 2, False)
kn_r = barrel(HB_SPLIT + GROOVE / 2, hw - 0.3, True)
kn_l = barrel(-hw + 0.3, -HB_SPLIT - GROOVE / 2, True)
kn_r = kn_r.faces(">X").edges("not <Z").edges("not <Y").fillet(KN_END_R)
kn_l = kn_l.faces("<X").edges("not <Z").edges("not <Y").fillet(KN_END_R)
upright = upright.union(mid).union(kn_r).union(kn_l)

# seam line between the upright and the middle barrel on the underside
upright = upright.cut(box_at(-HB_SPLIT + GROOVE / 2, HB_SPLIT - GROOVE / 2, T - 0.15, T + 0.2, -0.1, 0.5))

# ---- cartridge slot notch on the top / outer edge ----
upright = upright.cut(box_at(GBA_X - GBA_HALF, GBA_X + GBA_HALF, -1.0, GBA_Y, H - GBA_D, H + 1.0))

# finger scoop: cylinder along Y under the notch floor, as deep as the notch
scoop_r = (SCOOP_W / 2.0) ** 2 / (2.0 * SCOOP_D) + SCOOP_D / 2.0
scoop = (
    cq.Workplane("XZ", origin=(0, GBA_Y, 0))
    .center(SCOOP_X, H - GBA_D - SCOOP_D + scoop_r)
    .circle(scoop_r)
    .extrude(GBA_Y + 1.0)            # XZ normal is -Y: runs from GBA_Y to -1
)
upright = upright.cut(scoop)

# ---- stylus keyhole in the top face (+X end) ----
key = (
    cq.Workplane("XY", origin=(0, 0, H - KEY_DEPTH))
    .center(KEY_X, KEY_Y).circle(KEY_R).extrude(KEY_DEPTH + 1.0)
    .union(box_at(KEY_SLOT_X0, KEY_X, KEY_Y - KEY_SLOT_W / 2, KEY_Y + KEY_SLOT_W / 2, H - KEY_DEPTH, H + 1.0))
)
upright = upright.cut(key)

# ---- power slide switch in the top face (-X end) ----
upright = upright.cut(box_at(SW_X0, SW_X1, SW_Y0, SW_Y1, H - 2.0, H + 1.0))
upright = upright.union(box_at(SW_X0, SW_X0 + SW_KNOB_W, SW_Y0 + 0.1, SW_Y1 - 0.4, H - 2.0, H + SW_KNOB_UP))
upright = upright.union(box_at(SW_X0 + SW_KNOB_W - 0.1, SW_X1 - 0.2, SW_Y0 + 0.3, SW_Y1 - 0.6, H - 2.0, H + SW_PLATE_UP))

# ---- strap groove wrapping around the +X outer vertical edge ----
sr = STRAP_W / 2.0
strap = (
    box_at(STRAP_X0, hw + 5.0, -1.0, STRAP_END - sr, STRAP_ZC - sr, STRAP_ZC + sr)
    .union(cq.Workplane("YZ", origin=(STRAP_X0, 0, 0)).center(STRAP_END - sr, STRAP_ZC).circle(sr).extrude(15.0))
)
# keep only a constant-depth skin following the rounded corner
core = rounded_rect(cq.Workplane("XY"), -hw + STRAP_DEPTH, hw - STRAP_DEPTH, STRAP_DEPTH, T + 5,
                    R_OUT - STRAP_DEPTH, R_OUT - STRAP_DEPTH, 0, 0).extrude(H)
upright = upright.cut(strap.cut(core))

# ---- volume slider on the +X side ----
upright = upright.cut(box_at(hw - 1.2, hw + 2.0, VOL_Y[0], VOL_Y[1], VOL_Z[0], VOL_Z[1]))
upright = upright.union(box_at(hw - 1.2, VOL_KNOB_X1, VOL_Y[0] + 0.27, VOL_Y[1] - 0.27, VOL_KNOB_Z[0], VOL_KNOB_Z[1]))
yc = (VOL_Y[0] + VOL_Y[1]) / 2.0
nub = (
    cq.Workplane("YZ", origin=(VOL_KNOB_X1 - 0.1, 0, 0))
    .polyline([(yc - 1.1, VOL_KNOB_Z[1] - 0.7), (yc + 1.1, VOL_KNOB_Z[1] - 0.7), (yc, VOL_KNOB_Z[0] + 1.4)])
    .close()
    .extrude(VOL_NUB_X1 - VOL_KNOB_X1 + 0.1)
)
upright = upright.union(nub)


# ---- shoulder buttons: outlined by thin grooves at both lower corners ----
def shoulder_grooves(sign):
    g = GROOVE
    if sign > 0:
        outer = box_at(SH_X - g, hw + 2, -1, SH_Y + g, -1, SH_Z + g)
        inner = box_at(SH_X, hw + 3, -2, SH_Y, -2, SH_Z)
    else:
        outer = box_at(-hw - 2, -SH_X + g, -1, SH_Y + g, -1, SH_Z + g)
        inner = box_at(-hw - 3, -SH_X, -2, SH_Y, -2, SH_Z)
    shell = outer.cut(inner)
    skin = box_at(-hw + 2.0, hw - 2.0, 2.0, T - 2.0, 2.0, H - 2.0)
    return shell.cut(skin)


upright = upright.cut(shoulder_grooves(1)).cut(shoulder_grooves(-1))

# ---- underside: card slot cover, small window, LEDs ----
card = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .center(CARD_X, CARD_Y).rect(CARD_L, CARD_W).extrude(2.2)
    .edges("|Z").fillet(1.2)
)
upright = upright.cut(card)
win = (
    cq.Workplane("XY", origin=(0, 0, -0.1))
    .center(WIN_X, WIN_Y).rect(WIN_L, WIN_W).extrude(1.1)
    .edges("|Z").fillet(1.2)
)
upright = upright.cut(win)
for lx in LED_X:
    upright = upright.cut(
        cq.Workplane("XY", origin=(0, 0, -0.1)).center(lx, LED_Y).rect(LED_S, LED_S).extrude(1.1)
    )

# ---- inner face: screen recess and controls ----
scr_in = (
    cq.Workplane("XZ", origin=(0, T + 0.1, 0))
    .center(0, SCR_IN_Z).rect(SCR_W, SCR_H)
    .extrude(SCR_DEPTH + 0.1)
)
upright = upright.cut(scr_in)

face = cq.Workplane("XZ", origin=(0, T - 0.3, 0))   # extrude(-h) grows toward +Y
pad = (
    face.center(PAD_X, PAD_Z).rect(PAD_LEN, PAD_ARM).extrude(-(PAD_H + 0.3))
    .union(face.center(PAD_X, PAD_Z).rect(PAD_ARM, PAD_LEN).extrude(-(PAD_H + 0.3)))
)
pad = pad.faces(">Y").edges().fillet(0.4)
upright = upright.union(pad)

for dx, dz in ((0, ABXY_OFF), (0, -ABXY_OFF), (ABXY_OFF, 0), (-ABXY_OFF, 0)):
    btn = (
        face.center(ABXY_X + dx, ABXY_Z + dz)
        .circle(ABXY_R).extrude(-(ABXY_H + 0.3))
        .faces(">Y").edges().fillet(0.8)
    )
    upright = upright.union(btn)

for zz in SS_Z:
    b = (
        face.center(SS_X, zz)
        .circle(SS_R).extrude(-(SS_H + 0.3))
        .faces(">Y").edges().fillet(0.3)
    )
    upright = upright.union(b)

# =====================================================================
# Lid (flat half): rounded tray with a rim on three sides
# =====================================================================
lid_y0 = LID_Y0 - 1.0            # overlaps the hinge barrel by 1 mm
lid = box_at(-hw, hw, lid_y0, LID_Y1, 0.0, LID_T)
lid = lid.edges("|Z").edges(">Y").fillet(LID_R_CORNER)
lid = lid.faces("<Z").edges("not <Y").fillet(LID_R_BOT)
lid = lid.faces(">Z").edges("not <Y").fillet(LID_R_TOP)

pocket = (
    cq.Workplane("XY", origin=(0, 0, LID_T - RIM_DEPTH))
    .center(0, (lid_y0 - 2.0 + LID_Y1 - RIM_W) / 2.0)
    .rect(W - 2 * RIM_W, (LID_Y1 - RIM_W) - (lid_y0 - 2.0))
    .extrude(RIM_DEPTH + 1.0)
    .edges("|Z").edges(">Y").fillet(1.0)
    .faces("<Z").edges().fillet(FLOOR_FILLET)
)
lid = lid.cut(pocket)

floor_z = LID_T - RIM_DEPTH
lid = lid.cut(
    cq.Workplane("XY", origin=(0, 0, floor_z - SCR_DEPTH))
    .center(0, SCR_LID_Y).rect(SCR_W, SCR_H).extrude(2.0)
)
holes = (
    cq.Workplane("XY", origin=(0, 0, floor_z - 1.0))
    .pushPoints([(sx * cx, cy) for sx in (-1, 1) for cx in SPK_X for cy in SPK_Y])
    .circle(SPK_D / 2.0)
    .extrude(2.0)
)
lid = lid.cut(holes)

result = upright.union(lid)

VIEW = {"azimuth": 45, "elevation": 26}
